import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 160.0        # overall length (X) incl. end caps
W = 104.4        # overall width (Y) of the shell halves
H = 60.5         # overall height (Z)

E = 3.0          # end cap thickness (X)
CAP_INSET = 0.9  # end cap inset from the shell side faces (Y)
R_SHELL = 1.2    # radius on the long (X) edges of the shell
R_CAP_H = 2.0    # fillet on the top/bottom outer edges of the end panels

P = 2.4          # corner post width (Y); post depth = E
R_POST = 1.3     # radius on the outer vertical corner of each post
HEAD_H = 2.5     # height of the post heads (top and bottom)
R_HEAD = 1.0     # corner radius of the post heads
HEAD_PROUD = 0.4 # heads stand proud of the rods (Y)
R_HEAD_END = 0.5 # rounding of the exposed head end edges

GROOVE_W = 0.35  # mid-height split V-groove width (Z)
GROOVE_D = 0.25  # groove depth

SLOT_X = 1.7     # recess in each post head (X length)
SLOT_Y = 1.7     # recess width (Y)
SLOT_D = 1.6     # recess depth

VIEW = {"azimuth": 45, "elevation": 26}

Ls = L - 2 * E          # shell length
Wc = W - 2 * CAP_INSET  # end cap width

# ---------------- shell (top + bottom halves) ----------------
shell = cq.Workplane("XY").box(Ls, W, H).edges("|X").fillet(R_SHELL)

# mid-height split: V-groove along the front and back faces
for sy in (-1, 1):
    hw = GROOVE_W / 2 / GROOVE_D * (GROOVE_D + 0.5)
    tri = (
        cq.Workplane("YZ")
        .polyline([(sy * (W / 2 + 0.5), hw), (sy * (W / 2 - GROOVE_D), 0.0), (sy * (W / 2 + 0.5), -hw)])
        .close()
        .extrude(Ls + 2)
        .translate((-Ls / 2 - 1, 0, 0))
    )
    shell = shell.cut(tri)


# ---------------- end caps (panel between two corner posts) ----------------
def corner_post(sy):
    """Corner post of the +X end cap, local x from 0 (shell face) to E (outer face):
    a rounded rod with a squarer head at each end carrying a small recess."""
    yc = sy * (Wc / 2 - P / 2)
    sel = ">X and >Y" if sy > 0 else ">X and <Y"
    rod = (
        cq.Workplane("XY").box(E, P, H - 2 * HEAD_H).translate((E / 2, yc, 0))
        .edges("|Z").edges(sel).fillet(R_POST)
    )
    post = rod
    yh = sy * (Wc / 2 - P / 2 + HEAD_PROUD / 2)
    for sz in (-1, 1):
        head = (
            cq.Workplane("XY").box(E, P + HEAD_PROUD, HEAD_H)
            .translate((E / 2, yh, sz * (H / 2 - HEAD_H / 2)))
            .edges("|Z").edges(sel).fillet(R_HEAD)
        )
        # soften the exposed edges of the head end
        if R_HEAD_END > 0:
            zsel = ">Z" if sz > 0 else "<Z"
            y_in = sy * (Wc / 2 - P)
            head = head.faces(zsel).edges().filter(
                lambda e: e.Center().x > 1e-3 and abs(e.Center().y - y_in) > 1e-3
            ).fillet(R_HEAD_END)
        # recess in the end of the head
        head = head.cut(
            cq.Workplane("XY").box(SLOT_X, SLOT_Y, SLOT_D * 2).translate((E / 2 - 0.2, yh, sz * H / 2))
        )
        post = post.union(head)
    return post


def end_cap():
    wp = Wc - 2 * P
    panel = cq.Workplane("XY").box(E, wp, H).translate((E / 2, 0, 0))
    panel = panel.edges("|Y and >X").fillet(R_CAP_H)
    cap = panel
    for sy in (-1, 1):
        cap = cap.union(corner_post(sy))
    return cap


cap_r = end_cap().translate((Ls / 2, 0, 0))
cap_l = end_cap().mirror("YZ").translate((-Ls / 2, 0, 0))

result = shell.union(cap_r).union(cap_l)
